import math
import cadquery as cq

# =====================================================================
#  End plate / cover plate with moulded back pocket
#  X = width (left -> right seen from the front), Z = height, Y = thickness
#  front face at y = 0, back face at y = T
# =====================================================================

# ---------------- driving dimensions (mm) ----------------
T = 7.0            # plate thickness (Y)
CH = 2.0           # chamfer around the front face perimeter
WEB = 2.0          # web thickness left under the back pocket
CRES_K = 1.0       # slope (dz/dy) of the oblique cut that forms the front bottom arc

# outline (X right, Z up), counter-clockwise as seen from the front
P1 = (0.0, 23.4)    # left edge, bottom
P2 = (6.0, 17.4)    # end of bottom-left corner cut
P3 = (42.6, 17.4)   # kink of the bottom edge
P4 = (78.4, 0.0)    # bottom corner (start of corner cut)
P5 = (85.8, 2.7)    # bottom corner (end of corner cut)
P6 = (100.0, 32.5)  # right edge bottom
P7 = (100.0, 84.7)  # right edge top
P8 = (97.9, 86.6)   # top-right corner cut
P9 = (3.2, 86.6)    # top-left corner cut
P10 = (0.0, 83.4)   # left edge top
OUTLINE = [P1, P2, P3, P4, P5, P6, P7, P8, P9, P10]
# the small top-right corner cut is made after the front chamfer (front face corner stays sharp)
OUTLINE_SHARP = [P1, P2, P3, P4, P5, P6, (P7[0], P8[1]), P9, P10]

# front face bottom boundary: large circular arc
ARC_C = (24.24, -68.18)
ARC_R = 88.43

# back pocket: per outline edge (inset at back face, inset at pocket floor)
#   -> different values give a sloped (drafted) pocket wall
#   (a, b, inset at back face, inset at floor, inset of the ledge step)
POCKET_EDGES = [
    (P1, P2, 7.0, 7.0, 3.0),
    (P2, P3, 6.5, 6.5, 3.0),
    (P3, P4, 6.5, 6.5, 3.0),
    (P4, P5, 6.5, 6.5, 3.0),
    (P5, P6, 4.0, 4.0, 4.0),
    (P6, P7, 1.9, 1.9, 1.9),
    (P7, P8, 1.9, 1.9, 1.9),
    (P8, P9, 1.9, 1.9, 1.9),
    (P10, P1, 0.6, 8.0, 2.1),
]
LEDGE_H = 1.0                # ledge step below the back face along the bottom rim
LEFT_BLOCK = (4.5, 75.5)     # thick left rim at the top: width, lower Z
L_NOTCH = (46.5, 60.0, 3.0)  # recess in the sloped left rim: z0, z1, x0

# right-edge notches in the back rim (Z ranges), depth from the back, depth into X
R_NOTCH = [(54.3, 59.8), (47.0, 52.0)]
R_NOTCH_D = 2.7
R_NOTCH_X = 3.0
SHELF = (89.5, 34.7, 35.3)           # thin horizontal rib in the lower right pocket corner: x0, z0, z_top
DIAG_NOTCH = (13.5, 21.8, 2.0)       # recess in the lower-right diagonal rim: z0, z1, remaining rim
SLOT = ((79.4, 9.0), (85.8, 25.5), 1.4, 0.5)   # groove on the floor: start, end, width, depth
SLOT_PIN = (81.6, 15.9)

# front features
BIG_D = 8.0
BIG_DEPTH = 0.8
BIG_DRAFT = 0.3
BIG_POS = [(12.95, 79.7), (66.3, 79.7), (12.95, 27.7), (90.3, 29.8), (81.3, 10.3)]
DIMPLE_D = 2.9
DIMPLE_DEPTH = 0.75
DIMPLE_POS = [(6.84, 81.3), (47.6, 81.3), (72.7, 81.2), (2.6, 54.4),
              (6.5, 30.5), (53.9, 21.8), (90.4, 17.8)]
LABEL = (16.6, 61.1, 45.3, 60.0)   # x0, x1, z0, z1
LABEL_DEPTH = 0.45

# back floor features
BACK_RECT = [(68.9, 47.5), (93.5, 47.5), (93.5, 78.3), (87.1, 78.3), (87.1, 75.3), (68.9, 75.3)]
BACK_RECT_DEPTH = 0.4
PIN_POCKETS = [((74.3, 81.0), 5.6, 5.4), ((49.2, 81.0), 5.6, 5.4),
               ((55.8, 21.6), 5.0, 5.0), ((38.8, 53.7), 3.4, 8.2),
               ((9.0, 79.4), 2.4, 4.0), ((9.0, 29.9), 2.4, 5.0)]
PIN_POCKET_DEPTH = 0.5
PIN_HOLE_D = 2.2


def V(x, z, y=0.0):
    return cq.Vector(x, y, z)


def offset_polygon(edges, which):
    """vertices of the polygon bounded by the inward offset lines of the edges"""
    lines = []
    for (a, b, d_top, d_floor, d_ledge) in edges:
        d = {"top": d_top, "floor": d_floor, "ledge": d_ledge}[which]
        dx, dz = b[0] - a[0], b[1] - a[1]
        L = math.hypot(dx, dz)
        ux, uz = dx / L, dz / L
        nx, nz = -uz, ux            # inward normal for a CCW outline
        lines.append(((a[0] + nx * d, a[1] + nz * d), (ux, uz)))
    pts = []
    n = len(lines)
    for i in range(n):
        (p, u), (q, w) = lines[i - 1], lines[i]
        den = u[0] * w[1] - u[1] * w[0]
        t = ((q[0] - p[0]) * w[1] - (q[1] - p[1]) * w[0]) / den
        pts.append((p[0] + u[0] * t, p[1] + u[1] * t))
    return pts


def poly_wire(pts, y):
    return cq.Wire.makePolygon([V(x, z, y) for (x, z) in pts], close=True)


def prism(pts, y0, y1):
    """prism from an XZ polygon between y0 and y1"""
    return cq.Solid.extrudeLinear(cq.Face.makeFromWires(poly_wire(pts, y0)), cq.Vector(0, y1 - y0, 0))


def box(x0, x1, y0, y1, z0, z1):
    return cq.Solid.makeBox(x1 - x0, y1 - y0, z1 - z0, cq.Vector(x0, y0, z0))


# ---------------- base plate ----------------
outline_prism = prism(OUTLINE, 0.0, T)
body = prism(OUTLINE_SHARP, 0.0, T)

# ---------------- front bottom crescent: oblique circular cut ----------------
# a disc through the front bottom arc, swept obliquely backwards and downwards
y0 = -1.0
disc = cq.Face.makeFromWires(cq.Wire.makeCircle(ARC_R, V(ARC_C[0], ARC_C[1] + CRES_K * (-y0), y0),
                                                cq.Vector(0, 1, 0)))
cres = cq.Solid.extrudeLinear(disc, cq.Vector(0, T + 2.0, -CRES_K * (T + 2.0)))
body = body.cut(cres)

# ---------------- front perimeter chamfer (straight front edges) ----------------
front = [f for f in body.Faces() if f.geomType() == "PLANE" and abs(f.Center().y) < 1e-6][0]
ch_edges = [e for e in front.Edges() if e.geomType() == "LINE"]
body = body.chamfer(CH, None, ch_edges)
# top-right corner cut
body = body.cut(prism([P7, (P7[0] + 1, P7[1]), (P7[0] + 1, P8[1] + 1), (P8[0], P8[1] + 1), P8], -1.0, T + 1.0))

# ---------------- back pocket (drafted walls where insets differ) ----------------
top_pts = offset_polygon(POCKET_EDGES, "top")
floor_pts = offset_polygon(POCKET_EDGES, "floor")
pocket = cq.Solid.makeLoft([poly_wire(floor_pts, WEB), poly_wire(top_pts, T)], True)
pocket = pocket.fuse(prism(top_pts, T - 0.01, T + 1.0))
pocket = pocket.fuse(prism(offset_polygon(POCKET_EDGES, "ledge"), T - LEDGE_H, T + 1.0))
body = body.cut(pocket)

# thick left rim at the top (flat top)
lb = box(0.0, LEFT_BLOCK[0], WEB - 0.01, T, LEFT_BLOCK[1], 86.6).intersect(outline_prism)
body = body.fuse(lb)

# right rim: local pad, notches and the small tab between them
for (z0, z1) in R_NOTCH:
    body = body.cut(box(100.0 - R_NOTCH_X, 101.0, T - R_NOTCH_D, T + 1.0, z0, z1))
zt = 0.5 * (R_NOTCH[0][0] + R_NOTCH[1][1])
body = body.fuse(cq.Solid.makeCylinder(0.9, R_NOTCH_D - 0.3, V(100.0 - 0.6, zt, T - R_NOTCH_D + 0.3),
                                       cq.Vector(0, 1, 0)).intersect(outline_prism))

# recess in the sloped left rim
body = body.cut(box(L_NOTCH[2], 9.5, WEB, T + 1.0, L_NOTCH[0], L_NOTCH[1]))

# block (shelf) in the lower right corner of the pocket
sx0, sz0, sz1 = SHELF
body = body.fuse(box(sx0, 98.5, WEB - 0.01, T, sz0, sz1))


def along(a, b, t, d):
    """point at parameter t along a->b, moved inward by d"""
    dx, dz = b[0] - a[0], b[1] - a[1]
    L = math.hypot(dx, dz)
    return (a[0] + dx * t - dz / L * d, a[1] + dz * t + dx / L * d)


# recess into the inner side of the lower-right diagonal rim
z0, z1, rem = DIAG_NOTCH
t0 = (z0 - P5[1]) / (P6[1] - P5[1])
t1 = (z1 - P5[1]) / (P6[1] - P5[1])
dn = [along(P5, P6, t0, rem), along(P5, P6, t1, rem), along(P5, P6, t1, 6.0), along(P5, P6, t0, 6.0)]
body = body.cut(prism(dn, WEB, T + 1.0))
dm = along(P5, P6, 0.5 * (t0 + t1), rem + 0.9)
body = body.cut(cq.Solid.makeCylinder(0.45, 2.0, V(dm[0], dm[1], WEB - 1.0), cq.Vector(0, 1, 0)))

# groove on the floor near the diagonal, with a pin hole
(sa, sb, sw, sd) = SLOT
ux, uz = sb[0] - sa[0], sb[1] - sa[1]
L = math.hypot(ux, uz)
nx, nz = -uz / L * sw / 2, ux / L * sw / 2
body = body.cut(prism([(sa[0] + nx, sa[1] + nz), (sa[0] - nx, sa[1] - nz),
                       (sb[0] - nx, sb[1] - nz), (sb[0] + nx, sb[1] + nz)], WEB - sd, WEB + 0.01))
body = body.cut(cq.Solid.makeCylinder(0.9, 1.0, V(SLOT_PIN[0], SLOT_PIN[1], WEB - 0.9), cq.Vector(0, 1, 0)))

# ---------------- front features ----------------
for (x, z) in BIG_POS:
    body = body.cut(cq.Solid.makeCone(BIG_D / 2 + 0.01, BIG_D / 2 - BIG_DRAFT, BIG_DEPTH + 0.01,
                                      V(x, z, -0.01), cq.Vector(0, 1, 0)))
lx0, lx1, lz0, lz1 = LABEL
body = body.cut(box(lx0, lx1, -0.01, LABEL_DEPTH, lz0, lz1))
ds_r = ((DIMPLE_D / 2) ** 2 + DIMPLE_DEPTH ** 2) / (2 * DIMPLE_DEPTH)   # sphere radius
for (x, z) in DIMPLE_POS:
    body = body.cut(cq.Solid.makeSphere(ds_r, V(x, z, DIMPLE_DEPTH - ds_r), angleDegrees1=-90, angleDegrees2=90))

# ---------------- back floor features ----------------
body = body.cut(prism(BACK_RECT, WEB - BACK_RECT_DEPTH, WEB + 0.01))
for ((x, z), w, h) in PIN_POCKETS:
    body = body.cut(box(x - w / 2, x + w / 2, WEB - PIN_POCKET_DEPTH, WEB + 0.01, z - h / 2, z + h / 2))
    pd = min(PIN_HOLE_D, w - 0.6)
    body = body.fuse(cq.Solid.makeCylinder(pd / 2, PIN_POCKET_DEPTH + 0.8,
                                           V(x, z, WEB - PIN_POCKET_DEPTH - 0.01), cq.Vector(0, 1, 0)))

result = cq.Workplane("XY").add(body.clean())
